import math
import cadquery as cq

# ---------------------------------------------------------------
# Servo (XM430-like) with a sheet-metal side/bottom bracket
# Servo horn axis is +X, servo centred on the origin.
# ---------------------------------------------------------------

# servo body
SX, SY, SZ = 34.0, 46.5, 28.5
EDGE_CH = 2.0            # chamfer on the four long (X-parallel) edges
EAR_L = 2.8              # length (X) of the corner ears

# back cap (between servo and bracket flanges)
CAP_T = 3.2
CAP_Y = 48.0
CAP_Z = 30.2
CAP_CH = 2.0

# horn / idler axis
HORN_Y, HORN_Z = 11.9, 0.0
HORN_R, HORN_T = 10.25, 2.1
HUB_R, HUB_T = 3.9, 1.75
HORN_HOLE_PCD = 8.0

# bracket
T = 2.0                  # sheet thickness
RI = 2.0                 # inner bend radius
RO = RI + T
BY_OUT = 27.9            # outer half-width of bracket (Y)
Z_TOP = 13.3             # flat top of the side plates
X_DIAG0 = -14.1          # start of the 45 deg edge
X_FRONT = 11.1           # front (+X) edge of bracket
Z_BOT = -20.8            # outer bottom face
X_BP = -15.0             # -X end of the bottom plate
Z_BB = -13.7             # bottom of the rear flange
X_BO = -22.2             # outer face of rear flanges
FL_IN_Y = 16.8           # inner edge of rear flanges

# fasteners
FB_Y, FB_Z = 20.0, 11.0  # rear flange bolts (also servo corner holes)
FB_R, FB_H = 2.25, 2.6
BB_PCD = 8.0             # bottom plate bolt circle
BB_HEAD_R, BB_HEAD_H = 1.85, 2.0
BB_SHANK_R, BB_SHANK_H = 1.0, 2.0
BP_CENTER_HOLE_R = 4.8


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def cyl_x(x0, x1, y, z, r):
    return (cq.Workplane("YZ", origin=(x0, 0, 0))
            .center(y, z).circle(r).extrude(x1 - x0))


def cyl_z(z0, z1, x, y, r):
    return (cq.Workplane("XY", origin=(0, 0, z0))
            .center(x, y).circle(r).extrude(z1 - z0))


def cyl_y(y0, y1, x, z, r):
    # extrude along +Y from y0 to y1
    return (cq.Workplane("XZ", origin=(0, y1, 0))
            .center(x, z).circle(r).extrude(y1 - y0))


# ---------------------------------------------------------------- servo
hx, hy, hz = SX / 2, SY / 2, SZ / 2
servo = box(-hx, hx, -hy, hy, -hz, hz)

# long edges: 45 deg chamfer between the corner ears, round on the ears
EAR_X0 = hx - EAR_L       # inner X of the ears
EAR_FR = 2.5              # radius of the rounded outer edge of the ears
xc = EAR_X0 - 0.3
for sy in (-1, 1):
    for sz in (-1, 1):
        tri = (cq.Workplane("YZ", origin=(-xc, 0, 0))
               .polyline([(sy * (hy + 0.01), sz * (hz + 0.01)),
                          (sy * (hy - EDGE_CH), sz * (hz + 0.01)),
                          (sy * (hy + 0.01), sz * (hz - EDGE_CH))]).close()
               .extrude(2 * xc))
        servo = servo.cut(tri)
        for sx in (-1, 1):
            x0, x1 = (xc, hx + 1) if sx > 0 else (-hx - 1, -xc)
            cyl = cyl_x(x0, x1, sy * (hy - EAR_FR), sz * (hz - EAR_FR), EAR_FR)
            corner = box(x0, x1,
                         min(sy * (hy - EAR_FR), sy * (hy + 1)),
                         max(sy * (hy - EAR_FR), sy * (hy + 1)),
                         min(sz * (hz - EAR_FR), sz * (hz + 1)),
                         max(sz * (hz - EAR_FR), sz * (hz + 1)))
            servo = servo.cut(corner.cut(cyl))
try:
    servo = servo.faces(">X or <X").edges().fillet(0.5)
except Exception:
    pass

# corner ears: outlined by a shallow groove on the three outer faces
EAR_Y0 = 17.0             # inner |Y| of the ears
EAR_Z0 = 8.1              # inner |Z| of the ears
GW, GD, EAR_R = 0.6, 0.7, 1.6


def ear_block(x0, y0, z0, c):
    b = box(x0, hx + 2, y0, hy + 2, z0, hz + 2)
    return b.edges("|X").edges("<Y").edges("<Z").chamfer(c)


ear_in = ear_block(EAR_X0, EAR_Y0, EAR_Z0, EAR_R)
ear_out = ear_block(EAR_X0 - GW, EAR_Y0 - GW, EAR_Z0 - GW,
                    EAR_R + GW * (2 - math.sqrt(2)))
core = box(-hx + GD, hx - GD, -hy + GD, hy - GD, -hz + GD, hz - GD)
core = core.edges("|X").chamfer(EDGE_CH - GD * (2 - math.sqrt(2)))
groove = ear_out.cut(ear_in).cut(core)
grooves = groove.union(groove.mirror("YZ"))
grooves = grooves.union(grooves.mirror("XZ"))
grooves = grooves.union(grooves.mirror("XY"))
servo = servo.cut(grooves)

# top face: 4 holes and connector pocket
for x in (-6.0, 6.0):
    for y in (8.0, -16.0):
        servo = servo.cut(cyl_z(hz - 3, hz + 1, x, y, 1.0))
        servo = servo.cut(
            cq.Workplane("XY", origin=(x, y, hz - 0.3))
            .circle(1.0).workplane(offset=0.3).circle(1.3).loft())
# connector socket: shallow pocket open to the back + D-shaped slot
conn = box(-hx - 1, -10.9, -6.5, 3.0, hz - 0.6, hz + 1)
servo = servo.cut(conn)
slot = box(-15.3, -11.9, -6.1, 2.0, hz - 3.0, hz + 1)
slot = slot.edges("|Z").edges("<X").fillet(1.4)
servo = servo.cut(slot)

# side faces: mounting holes (-Y face 2x2, +Y face only the +X column)
for x in (-6.0, 6.0):
    for z in (-8.0, 8.0):
        servo = servo.cut(cyl_y(-hy - 1, -hy + 3, x, z, 1.3))
for z in (-8.0, 8.0):
    servo = servo.cut(cyl_y(hy - 3, hy + 1, 6.0, z, 1.3))
# small slit on the +Y face
servo = servo.cut(box(10.5, 14.4, hy - 0.4, hy + 1, -0.15, 0.15))

# +X face: corner through holes with counterbores
for y in (-FB_Y, FB_Y):
    for z in (-FB_Z, FB_Z):
        servo = servo.cut(cyl_x(-hx - 1, hx + 1, y, z, 1.0))
        servo = servo.cut(cyl_x(hx - 0.6, hx + 1, y, z, 1.6))

# +X face: two small holes left of the horn
for z in (-FB_Z, FB_Z):
    servo = servo.cut(cyl_x(hx - 3, hx + 1, 4.0, z, 1.2))

# +X face: label recess
label = (cq.Workplane("YZ", origin=(hx - 0.4, 0, 0))
         .center(-17.75, 0).rect(7.9, 14.0).extrude(1)
         .edges("|X").fillet(1.0))
servo = servo.cut(label)

# ---------------------------------------------------------------- horn
horn = cyl_x(hx, hx + HORN_T, HORN_Y, HORN_Z, HORN_R)
for k in range(8):
    a = math.radians(45 * k)
    r = 1.2 if k % 2 == 0 else 0.9
    horn = horn.cut(cyl_x(hx - 0.1, hx + HORN_T + 0.1,
                          HORN_Y + HORN_HOLE_PCD * math.cos(a),
                          HORN_Z + HORN_HOLE_PCD * math.sin(a), r))
hub = cyl_x(hx + HORN_T, hx + HORN_T + HUB_T, HORN_Y, HORN_Z, HUB_R)
hub = hub.faces(">X").edges().chamfer(0.3)
horn = horn.union(hub)

# recessed screw below the horn (counterbore with cross-head screw inside)
SCR_Z = -11.9
servo = servo.cut(cyl_x(hx - 1.4, hx + 1, HORN_Y, SCR_Z, 1.8))
for w, h in ((2.0, 0.45), (0.45, 2.0)):
    servo = servo.cut(box(hx - 2.0, hx - 1.3, HORN_Y - w / 2, HORN_Y + w / 2,
                          SCR_Z - h / 2, SCR_Z + h / 2))

# ---------------------------------------------------------------- back cap
cap = box(-hx - CAP_T, -hx, -CAP_Y / 2, CAP_Y / 2, -CAP_Z / 2, CAP_Z / 2)
cap = cap.edges("|X").chamfer(CAP_CH)
xb = -hx - CAP_T
# idler pocket + idler disc with hub and square drive socket
cap = cap.cut(cyl_x(xb - 1, xb + 1.6, HORN_Y, HORN_Z, HORN_R))
idler = cyl_x(xb + 0.8, xb + 1.6, HORN_Y, HORN_Z, 8.6)
for k in range(8):
    a = math.radians(45 * k + 22.5)
    idler = idler.cut(cyl_x(xb, xb + 1.7, HORN_Y + 6.8 * math.cos(a),
                            HORN_Z + 6.8 * math.sin(a), 0.95))
idler = idler.union(cyl_x(xb + 0.3, xb + 1.6, HORN_Y, HORN_Z, 3.9))
idler = idler.cut(cyl_x(xb, xb + 0.7, HORN_Y, HORN_Z, 3.3))
idler = idler.union(cyl_x(xb + 0.5, xb + 1.6, HORN_Y, HORN_Z, 2.6))
idler = idler.cut(box(xb, xb + 2.5, HORN_Y - 1.2, HORN_Y + 1.2, -1.2, 1.2))
cap = cap.union(idler)

# ---------------------------------------------------------------- bracket
BY_IN = BY_OUT - T
YB = BY_OUT - RO            # bend axis Y (both bends)
XV = X_BO + RO              # vertical bend axis X
ZH = Z_BOT + RO             # horizontal bend axis Z

side_pts = [
    (XV, Z_TOP),
    (X_DIAG0, Z_TOP),
    (X_FRONT, Z_TOP - (X_FRONT - X_DIAG0)),
    (X_FRONT, ZH),
    (X_BP, ZH),
    (X_BP, Z_BB - (X_BP - (X_BO + 5.1))),
    (X_BO + 5.1, Z_BB),
    (XV, Z_BB),
]

bracket = None
for s in (-1, 1):
    # flat side plate
    y0 = s * BY_IN if s > 0 else -BY_OUT
    plate = (cq.Workplane("XZ", origin=(0, y0 + T, 0))
             .polyline(side_pts).close().extrude(T))
    # vertical bend (around Z) to the rear flange
    vb = (cq.Workplane("XY", origin=(XV, s * YB, Z_BB))
          .circle(RO).circle(RI).extrude(Z_TOP - Z_BB))
    vb = vb.intersect(box(XV - RO - 0.01, XV, 0 if s > 0 else -BY_OUT - 1,
                          BY_OUT + 1 if s > 0 else 0, Z_BB - 1, Z_TOP + 1))
    vb = vb.intersect(box(XV - RO - 1, XV + 1,
                          s * YB if s > 0 else -BY_OUT - 1,
                          BY_OUT + 1 if s > 0 else s * YB, Z_BB - 1, Z_TOP + 1))
    # rear flange
    fl = box(X_BO, X_BO + T, min(s * FL_IN_Y, s * YB), max(s * FL_IN_Y, s * YB),
             Z_BB, Z_TOP)
    fl = fl.edges("|X").edges("<Y" if s > 0 else ">Y").fillet(0.6)
    # horizontal bend (around X) to the bottom plate
    hb = (cq.Workplane("YZ", origin=(X_BP, 0, 0)).center(s * YB, ZH)
          .circle(RO).circle(RI).extrude(X_FRONT - X_BP))
    hb = hb.intersect(box(X_BP - 1, X_FRONT + 1,
                          s * YB if s > 0 else -BY_OUT - 1,
                          BY_OUT + 1 if s > 0 else s * YB, ZH - RO - 1, ZH))
    part = plate.union(vb).union(fl).union(hb)
    bracket = part if bracket is None else bracket.union(part)

bottom = box(X_BP, X_FRONT, -YB, YB, Z_BOT, Z_BOT + T)
bracket = bracket.union(bottom)

# centre hole of the horn-mount pattern in the bottom plate
BB_X, BB_Y = 0.0, HORN_Y
bracket = bracket.cut(cyl_z(Z_BOT - 1, Z_BOT + T + 1, BB_X, BB_Y, BP_CENTER_HOLE_R))

# ---------------------------------------------------------------- fasteners
fasteners = None


def add(f):
    global fasteners
    fasteners = f if fasteners is None else fasteners.union(f)


for y in (-FB_Y, FB_Y):
    for z in (-FB_Z, FB_Z):
        b = cyl_x(X_BO - FB_H, X_BO, y, z, FB_R)
        b = b.faces("<X").edges().fillet(0.4)
        b = b.cut(cq.Workplane("YZ", origin=(X_BO - FB_H - 0.1, 0, 0))
                  .center(y, z).polygon(6, 2.3).extrude(1.3))
        add(b)

for k in range(8):
    a = math.radians(22.5 + 45 * k)
    x = BB_X + BB_PCD * math.cos(a)
    y = BB_Y + BB_PCD * math.sin(a)
    head = cyl_z(Z_BOT + T, Z_BOT + T + BB_HEAD_H, x, y, BB_HEAD_R)
    head = head.faces(">Z").edges().fillet(0.3)
    sh = cyl_z(Z_BOT - BB_SHANK_H, Z_BOT + 0.5, x, y, BB_SHANK_R)
    sh = sh.faces("<Z").edges().chamfer(0.2)
    add(head.union(sh))

result = (servo.union(horn).union(cap)
          .union(bracket).union(fasteners))

VIEW = {"azimuth": 45, "elevation": 26}
